import cadquery as cq
import math

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
BODY_D = 60.0        # main cap diameter
BODY_H = 50.2        # main cap height (above thread stub)
TOP_FILLET = 5.0     # rounding of the top edge
SEAM_ANGLE = -70.0   # angular position of the cylinder seam

THREAD_H = 6.2       # height of the threaded stub below the body
THREAD_CREST_R = 24.9
THREAD_ROOT_R = 22.8
THREAD_PITCH = 3.65
THREAD_PHASE = 1.0   # axial shift of the helix start (mm)

HOLE_D = 20.0        # central recess in the underside of the stub
HOLE_DEPTH = 6.2     # depth of the cylindrical wall (up to the body plane)
CONE_RISE = 2.5      # conical floor rising back toward the opening

# ---------------- main body ----------------
body = (
    cq.Workplane("XY")
    .circle(BODY_D / 2.0)
    .extrude(BODY_H)
    .faces(">Z")
    .edges()
    .fillet(TOP_FILLET)
    .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
)

# ---------------- threaded stub ----------------
core = (
    cq.Workplane("XY")
    .workplane(offset=-THREAD_H)
    .circle(THREAD_ROOT_R)
    .extrude(THREAD_H + 0.5)
)

# helical V thread, swept along a helix, then trimmed to the stub height
ext = THREAD_PITCH * 1.5
helix_h = THREAD_H + 2 * ext
r0 = THREAD_ROOT_R - 0.4
depth = THREAD_CREST_R - r0
half_base = 0.46 * THREAD_PITCH
half_tip = 0.05 * THREAD_PITCH
helix = cq.Wire.makeHelix(THREAD_PITCH, helix_h, r0)
path = cq.Workplane("XY").newObject([helix])
profile = (
    cq.Workplane("XZ")
    .polyline([
        (r0, -half_base),
        (r0 + depth, -half_tip),
        (r0 + depth, half_tip),
        (r0, half_base),
    ])
    .close()
)
thread = profile.sweep(path, isFrenet=True)
thread = thread.translate((0, 0, -THREAD_H - ext + THREAD_PHASE))

trim = (
    cq.Workplane("XY")
    .workplane(offset=-THREAD_H)
    .rect(3 * BODY_D, 3 * BODY_D)
    .extrude(THREAD_H)
)
thread = thread.intersect(trim)

stub = core.union(thread)

result = body.union(stub)

# ---------------- central recess with a conical floor ----------------
# the floor is a shallow cone whose tip points back toward the opening
z_mouth = -THREAD_H
z_rim = z_mouth + HOLE_DEPTH
r_h = HOLE_D / 2.0
z_tip = z_rim - CONE_RISE
recess = (
    cq.Workplane("XZ")
    .polyline([
        (0.0, z_mouth - 1.0),
        (r_h, z_mouth - 1.0),
        (r_h, z_rim),
        (0.0, z_tip),
    ])
    .close()
    .revolve(360.0, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), -90.0)
)
result = result.cut(recess)
